import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 200.0          # overall length (Y) of the stadium body at the back
H = 55.0           # overall height (Z) at the back
D = 55.0           # overall depth (X), back face -> front face
R = H / 2.0        # stadium end radius at the back
S = L - H          # straight length of the stadium centre segment
RF = 10.0          # back edge round
TAPER = 5.7        # inward offset of the outline at the front face
RIM = 3.4          # width of the rim (top/bottom) around the front recess
RIM_END = 3.2      # width of the rim at the rounded ends
REC_DZ = -0.9      # recess sits slightly low in the front face
REC_DEPTH = 1.0    # depth of the front recess
FLOOR_IN = 1.7     # sloped recess wall width (top/bottom, average)
FLOOR_IN_END = 2.6 # sloped recess wall width at the rounded ends
FRONT_FIL = 2.0    # round on the outer front edge

# top vent slots
N_SLOTS = 19
SLOT_PITCH = 6.7
SLOT_W = 2.2
SLOT_LEN = 18.4
SLOT_XC = 0.455 * D     # slot centre measured from the back face
SLOT_DEPTH = 3.0       # floor depth of the shallow front part of a slot
SLOT_LIP = 0.5         # round on the slot openings
SLOT_DEEP = 6.0        # depth of the deep rear part of a slot
SLOT_DEEP_FRAC = 0.72  # fraction of the slot length that is deep

# bottom pad with slots and tripod boss
PAD_X0 = 15.0
PAD_X1 = 37.0
PAD_LEN = 132.0
PAD_DROP = 0.4     # pad stands slightly proud of the lowest body line
PAD_T = 3.0
BOT_SLOT_LEN = 19.0
BOT_SLOT_W = 2.0
BOT_SLOT_XC = 25.5
BOSS_R = 8.5
BOSS_REC_DEPTH = 0.8
BOSS_HOLE_DEPTH = 18.0
TEAR_K = 1.6
BOSS_HOLE_D = 7.0

# small flat on the top-back edge with a pin hole
FLAT_X0 = 5.8
FLAT_X1 = 14.8
FLAT_LEN = 42.0
FLAT_DEPTH = 0.6
PIN_HOLE_D = 1.5
PIN_HOLE_Y = 9.3

# back mounting holes
BACK_HOLE_Y = 51.0
BACK_HOLE_D = 4.5

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- side profile (X-Z), r(x) ----------------
# top: back round RF, then a large arc falling by TAPER at the front face
RA = ((D - RF) ** 2 + TAPER ** 2) / (2.0 * TAPER)   # radius of the falling arc
RT = R - TAPER                                         # stadium radius at the front


def r_of_x(x):
    if x <= RF:
        return R
    return R - RA + math.sqrt(RA ** 2 - (x - RF) ** 2)


def half_profile(wp):
    # closed half profile in local (x=X, y=Z) coords, z >= 0
    xm = RF + (D - RF) * 0.5
    return (
        wp.moveTo(0, 0)
        .lineTo(0, R - RF)
        .radiusArc((RF, R), RF)
        .threePointArc((xm, r_of_x(xm)), (D, RT))
        .lineTo(D, 0)
        .close()
    )


def full_profile(wp):
    xm = RF + (D - RF) * 0.5
    return (
        wp.moveTo(0, -(R - RF))
        .lineTo(0, R - RF)
        .radiusArc((RF, R), RF)
        .threePointArc((xm, r_of_x(xm)), (D, RT))
        .lineTo(D, -RT)
        .threePointArc((xm, -r_of_x(xm)), (RF, -R))
        .radiusArc((0, -(R - RF)), RF)
        .close()
    )


# middle straight part: extrude the full side profile along Y
mid = full_profile(cq.Workplane("XZ", origin=(0, S / 2.0, 0))).extrude(S)

# rounded ends: revolve the half profile 180 deg about the X axis
end_p = half_profile(cq.Workplane("XZ", origin=(0, S / 2.0, 0))).revolve(
    180, (0, 0, 0), (1, 0, 0)
)
bb = end_p.val().BoundingBox()
if bb.ymin < S / 2.0 - 1e-3:
    end_p = end_p.mirror("XZ", basePointVector=(0, S / 2.0, 0))
end_n = end_p.mirror("XZ")

body = mid.union(end_p).union(end_n).clean()

# front edge round
try:
    body = body.faces(">X").edges().fillet(FRONT_FIL)
except Exception:
    pass

# ---------------- front recess ----------------
rec_r = RT - RIM                          # recess outline radius at the face
rec_len = S + 2.0 * (RT - RIM_END)        # recess outline overall length
fl_r = rec_r - FLOOR_IN                   # flat floor (grille panel) radius
fl_len = rec_len - 2.0 * FLOOR_IN_END     # flat floor overall length
ext = 0.5                                 # extend the cutter past the face
k = (REC_DEPTH + ext) / REC_DEPTH
recess = (
    cq.Workplane("YZ", origin=(D - REC_DEPTH, 0, 0))
    .slot2D(fl_len, 2.0 * fl_r, 0)
    .workplane(offset=REC_DEPTH + ext)
    .center(0, REC_DZ * k)
    .slot2D(fl_len + (rec_len - fl_len) * k, 2.0 * (fl_r + (rec_r - fl_r) * k), 0)
    .loft(ruled=True)
)
body = body.cut(recess)

# ---------------- top vent slots ----------------
ys = [(i - (N_SLOTS - 1) / 2.0) * SLOT_PITCH for i in range(N_SLOTS)]
top_slots = (
    cq.Workplane("XY", origin=(0, 0, R - SLOT_DEPTH))
    .pushPoints([(SLOT_XC, y) for y in ys])
    .slot2D(SLOT_LEN, SLOT_W, 0)
    .extrude(SLOT_DEPTH + 2.0)
)
deep_len = SLOT_LEN * SLOT_DEEP_FRAC
deep_xc = SLOT_XC - SLOT_LEN / 2.0 + deep_len / 2.0
top_deep = (
    cq.Workplane("XY", origin=(0, 0, R - SLOT_DEEP))
    .pushPoints([(deep_xc, y) for y in ys])
    .slot2D(deep_len, SLOT_W, 0)
    .extrude(SLOT_DEEP)
)
top_slots = top_slots.union(top_deep)
body = body.cut(top_slots)

x_lo = SLOT_XC - SLOT_LEN / 2.0 - 0.2
x_hi = SLOT_XC + SLOT_LEN / 2.0 + 0.2
y_hi = max(ys) + SLOT_W


def _slot_lip(e):
    bb = e.BoundingBox()
    return (bb.zmin > R - SLOT_DEPTH + 0.3 and bb.xmin > x_lo and bb.xmax < x_hi
            and abs(bb.ymin) < y_hi and abs(bb.ymax) < y_hi)


try:
    lip_edges = [e for e in body.edges().vals() if _slot_lip(e)]
    body = body.newObject([body.val()]).newObject(lip_edges).fillet(SLOT_LIP)
except Exception as exc:
    print("slot lip fillet skipped:", exc)

# ---------------- bottom pad, slots and tripod boss ----------------
pad = (
    cq.Workplane("XY", origin=(0, 0, -R - PAD_DROP))
    .center((PAD_X0 + PAD_X1) / 2.0, 0)
    .rect(PAD_X1 - PAD_X0, PAD_LEN)
    .extrude(PAD_T + PAD_DROP)
    .edges("|Z")
    .fillet(2.0)
)
body = body.union(pad)

mid_i = (N_SLOTS - 1) // 2
bot_pts = [(BOT_SLOT_XC, ys[i]) for i in range(N_SLOTS) if abs(i - mid_i) > 1]
bot_slots = (
    cq.Workplane("XY", origin=(0, 0, -R - PAD_DROP - 1.0))
    .pushPoints(bot_pts)
    .slot2D(BOT_SLOT_LEN, BOT_SLOT_W, 0)
    .extrude(SLOT_DEPTH + 1.0)
)
body = body.cut(bot_slots)

bx_lo = BOT_SLOT_XC - BOT_SLOT_LEN / 2.0 - 0.2
bx_hi = BOT_SLOT_XC + BOT_SLOT_LEN / 2.0 + 0.2
z_pad = -R - PAD_DROP


def _bot_lip(e):
    bb = e.BoundingBox()
    return (bb.zmax < z_pad + 0.3 and bb.xmin > bx_lo and bb.xmax < bx_hi
            and max(abs(bb.ymin), abs(bb.ymax)) < y_hi
            and min(abs(bb.ymin), abs(bb.ymax)) > 2.0 * SLOT_PITCH - BOT_SLOT_W)


try:
    lip_edges = [e for e in body.edges().vals() if _bot_lip(e)]
    body = body.newObject([body.val()]).newObject(lip_edges).fillet(SLOT_LIP)
except Exception as exc:
    print("bottom slot lip fillet skipped:", exc)

boss_z0 = -R - PAD_DROP - 1.0
boss_cx = BOT_SLOT_XC
tear_d = BOSS_R * TEAR_K                      # apex distance of the tear-drop
phi = math.acos(BOSS_R / tear_d)
tear_pts = [
    (boss_cx - tear_d, 0.0),
    (boss_cx - BOSS_R * math.cos(phi), BOSS_R * math.sin(phi)),
    (boss_cx, 0.0),
    (boss_cx - BOSS_R * math.cos(phi), -BOSS_R * math.sin(phi)),
]
boss_rec = (
    cq.Workplane("XY", origin=(0, 0, boss_z0))
    .center(boss_cx, 0)
    .circle(BOSS_R)
    .extrude(1.0 + BOSS_REC_DEPTH)
    .union(
        cq.Workplane("XY", origin=(0, 0, boss_z0))
        .polyline(tear_pts)
        .close()
        .extrude(1.0 + BOSS_REC_DEPTH)
    )
)
body = body.cut(boss_rec)
boss_hole = (
    cq.Workplane("XY", origin=(boss_cx, 0, boss_z0))
    .circle(BOSS_HOLE_D / 2.0)
    .extrude(BOSS_HOLE_DEPTH + 1.0)
)
body = body.cut(boss_hole)

# ---------------- top-back flat with pin hole ----------------
flat_xc = 0.5 * (FLAT_X0 + FLAT_X1)
flat_pl = cq.Plane(origin=(flat_xc, 0, R - FLAT_DEPTH), xDir=(0, 1, 0), normal=(0, 0, 1))
flat_cut = (
    cq.Workplane(flat_pl)
    .slot2D(FLAT_LEN, FLAT_X1 - FLAT_X0, 0)
    .extrude(6.0)
)
body = body.cut(flat_cut)
pin = (
    cq.Workplane(flat_pl)
    .center(PIN_HOLE_Y, 0)
    .circle(PIN_HOLE_D / 2.0)
    .extrude(-4.0)
)
body = body.cut(pin)

# ---------------- back mounting holes ----------------
back_holes = (
    cq.Workplane("YZ", origin=(-1.0, 0, 0))
    .pushPoints([(-BACK_HOLE_Y, 0), (BACK_HOLE_Y, 0)])
    .circle(BACK_HOLE_D / 2.0)
    .extrude(16.0)
)
body = body.cut(back_holes)

# centre the part on the origin in X
result = body.translate((-D / 2.0, 0, 0))
